import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 62.8          # outer width  (X)
L = 100.0         # outer length (Y)
H = 20.6          # outer height (Z)
R_CORNER = 12.0   # outer vertical corner radius
T_WALL = 3.05     # wall thickness (below the lid seat)
T_FLOOR = 2.0     # floor thickness
CH_BOTTOM = 1.0   # bottom outer edge chamfer
R_FLOOR = 0.5     # inner floor / wall fillet

# lid seat on the inner side of the rim
T_LIP = 2.3       # wall thickness of the upper lip
LIP_D = 1.5       # depth of the vertical lip face
SEAT_CH = T_WALL - T_LIP   # 45 deg chamfer joining lip and wall
R_RIM = 0.3       # rounding on the inner top edge of the lip

# screw bosses
BOSS_OFF = 10.75  # boss centre distance from outer edges
BOSS_D = 4.6
BOSS_TOP = 4.3    # boss top height (absolute Z)
BOSS_HOLE = 1.7
BOSS_FIL = 1.8

# front (-Y) wall: recessed stadium slot + top notch
FS_X, FS_Z = 1.0, 8.15
FS_REC_L, FS_REC_H, FS_REC_D = 12.1, 6.6, 2.0
FS_REC_R = 0.3   # rounding of the recess rim
FS_SLOT_L, FS_SLOT_H = 9.5, 3.9
NOTCH_X = 0.65
NOTCH_TOP, NOTCH_BOT, NOTCH_D = 15.1, 11.2, 3.0
NOTCH_DEPTH = 0.9   # pocket depth into the wall (from outside)
NOTCH_R = 0.8       # rounding of the notch bottom corners

# right (+X) wall: vent grid
GRID_NY, GRID_NZ = 5, 4
GRID_PY, GRID_PZ = 2.78, 2.74
GRID_HOLE = 1.7
GRID_Y, GRID_Z = 25.9, 11.25

# left (-X) wall: rectangular port + small stadium slot
RECT_Y, RECT_Z, RECT_W, RECT_H = 0.5, 13.9, 12.8, 6.6
LS_Y, LS_Z, LS_L, LS_H = 26.6, 15.15, 11.0, 3.5
LS_REC_M, LS_REC_D = 0.3, 0.85   # shallow outer recess around the side slot


def rounded_box(w, l, r, z0, h):
    return (
        cq.Workplane("XY")
        .workplane(offset=z0)
        .rect(w, l)
        .extrude(h)
        .edges("|Z")
        .fillet(r)
    )


# ---------------- body ----------------
outer = rounded_box(W, L, R_CORNER, 0, H).faces("<Z").edges().chamfer(CH_BOTTOM)

# main cavity
wi, li, ri = W - 2 * T_WALL, L - 2 * T_WALL, R_CORNER - T_WALL
cavity = rounded_box(wi, li, ri, T_FLOOR, H).faces("<Z").edges().fillet(R_FLOOR)
body = outer.cut(cavity)

# lid seat: thinner upper lip with a 45 deg chamfer down to the wall
wl, ll, rl = W - 2 * T_LIP, L - 2 * T_LIP, R_CORNER - T_LIP
z_seat = H - LIP_D - SEAT_CH
seat = rounded_box(wl, ll, rl, z_seat, H - z_seat + 1).faces("<Z").edges().chamfer(SEAT_CH)
body = body.cut(seat)

# round the inner top edge of the lip
body = body.edges(
    cq.selectors.BoxSelector(
        (-wl / 2 - 0.05, -ll / 2 - 0.05, H - 0.05),
        (wl / 2 + 0.05, ll / 2 + 0.05, H + 0.05),
        boundingbox=True,
    )
).fillet(R_RIM)

# ---------------- screw bosses ----------------
bx, by = W / 2 - BOSS_OFF, L / 2 - BOSS_OFF
pts = [(sx * bx, sy * by) for sx in (-1, 1) for sy in (-1, 1)]
bosses = (
    cq.Workplane("XY")
    .workplane(offset=T_FLOOR - 0.5)
    .pushPoints(pts)
    .circle(BOSS_D / 2)
    .extrude(BOSS_TOP - T_FLOOR + 0.5)
)
body = body.union(bosses)
# fillet boss bases (only the circular root edges of the four bosses)
root_edges = []
for px, py in pts:
    root_edges += body.edges(
        cq.selectors.BoxSelector(
            (px - BOSS_D / 2 - 0.05, py - BOSS_D / 2 - 0.05, T_FLOOR - 0.01),
            (px + BOSS_D / 2 + 0.05, py + BOSS_D / 2 + 0.05, T_FLOOR + 0.01),
            boundingbox=True,
        )
    ).vals()
body = body.newObject(root_edges).fillet(BOSS_FIL)
holes = (
    cq.Workplane("XY")
    .workplane(offset=T_FLOOR)
    .pushPoints(pts)
    .circle(BOSS_HOLE / 2)
    .extrude(H)
)
body = body.cut(holes)

# ---------------- front (-Y) wall ----------------
# XZ workplane normal is -Y: positive extrude goes towards -Y
rec = (
    cq.Workplane("XZ", origin=(0, -L / 2 + FS_REC_D, 0))
    .center(FS_X, FS_Z)
    .slot2D(FS_REC_L, FS_REC_H)
    .extrude(FS_REC_D + 1)
)
body = body.cut(rec)
body = body.edges(
    cq.selectors.BoxSelector(
        (FS_X - FS_REC_L / 2 - 0.1, -L / 2 - 0.05, FS_Z - FS_REC_H / 2 - 0.1),
        (FS_X + FS_REC_L / 2 + 0.1, -L / 2 + 0.05, FS_Z + FS_REC_H / 2 + 0.1),
        boundingbox=True,
    )
).fillet(FS_REC_R)
slot = (
    cq.Workplane("XZ", origin=(0, -L / 2 + T_WALL + 1, 0))
    .center(FS_X, FS_Z)
    .slot2D(FS_SLOT_L, FS_SLOT_H)
    .extrude(T_WALL + 3)
)
body = body.cut(slot)

n_ext = (NOTCH_TOP - NOTCH_BOT) / 2 / NOTCH_D  # side slope, extended 1 mm above the rim
notch = (
    cq.Workplane("XZ", origin=(0, -L / 2 + NOTCH_DEPTH, 0))
    .polyline(
        [
            (NOTCH_X - NOTCH_TOP / 2 - n_ext, H + 1.0),
            (NOTCH_X + NOTCH_TOP / 2 + n_ext, H + 1.0),
            (NOTCH_X + NOTCH_BOT / 2, H - NOTCH_D),
            (NOTCH_X - NOTCH_BOT / 2, H - NOTCH_D),
        ]
    )
    .close()
    .extrude(NOTCH_DEPTH + 1)
    .edges("|Y")
    .edges("<Z")
    .fillet(NOTCH_R)
)
body = body.cut(notch)

# ---------------- right (+X) wall vent grid ----------------
gpts = []
for i in range(GRID_NY):
    for j in range(GRID_NZ):
        gpts.append(
            (GRID_Y + (i - (GRID_NY - 1) / 2) * GRID_PY,
             GRID_Z + (j - (GRID_NZ - 1) / 2) * GRID_PZ)
        )
grid = (
    cq.Workplane("YZ", origin=(W / 2 - T_WALL - 1, 0, 0))
    .pushPoints(gpts)
    .circle(GRID_HOLE / 2)
    .extrude(T_WALL + 3)
)
body = body.cut(grid)

# ---------------- left (-X) wall ----------------
rect_port = (
    cq.Workplane("YZ", origin=(-W / 2 - 1, 0, 0))
    .center(RECT_Y, RECT_Z)
    .rect(RECT_W, RECT_H)
    .extrude(T_WALL + 3)
)
body = body.cut(rect_port)

ls_rec = (
    cq.Workplane("YZ", origin=(-W / 2 - 1, 0, 0))
    .center(LS_Y, LS_Z)
    .slot2D(LS_L + 2 * LS_REC_M, LS_H + 2 * LS_REC_M)
    .extrude(1 + LS_REC_D)
)
body = body.cut(ls_rec)
ls_slot = (
    cq.Workplane("YZ", origin=(-W / 2 - 1, 0, 0))
    .center(LS_Y, LS_Z)
    .slot2D(LS_L, LS_H)
    .extrude(T_WALL + 3)
)
body = body.cut(ls_slot)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
